import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# rectangular tube (global coordinates, bottom at z = 0)
BOX_L, BOX_W, BOX_H = 50.0, 20.0, 9.0
OPEN_W, OPEN_H = 16.2, 3.4                    # through opening along x
SLOT_L, SLOT_W = 45.0, 10.8                   # slot in the bottom wall
WALL_B = (BOX_H - OPEN_H) / 2.0

# legs joining tube and lever frame
LEG_X0, LEG_X1 = 17.8, 20.7                   # |x| range of the legs
LEG_Y1 = 15.5                                 # back face of the leg blocks
LEG_H = 9.4

# lever frame: modelled flat in a local system, then tilted about the pin axis
PIV_Y, PIV_Z = 22.6, 7.6                      # pin axis (pivot)
TILT = 13.0                                   # lever tilt (deg)
FR_Y0 = 19.45                                 # frame front edge
FR_X = 20.6                                   # frame half width at the front
PL_Z0, PL_Z1 = 6.2, 7.6                       # thin plate bottom / top

HOLE_Y, HOLE_R, RING_R = 25.0, 2.2, 3.35
PIN_X, PIN_R, KNOB_R = 10.9, 1.1, 2.1

POCK_X0, POCK_X1, POCK_Y1 = 4.6, 9.3, 22.8     # front pockets (|x|, back edge)
BLK_XL, BLK_XR = 13.0, 11.5                   # inner faces of the left / right blocks
BLOCK_Y0 = 23.8                               # front face of the side blocks
WALL_TOP = 14.1                               # top of side blocks / walls
BR_X, BR_Y0, BR_Y1, BR_Z = 13.0, 30.0, 32.3, 14.1   # bridge between the arms
BR_FIL = 1.0                                  # rounding of the bridge front edge
RAMP_Y0 = 28.4                                # start of the ramp up to the bridge
U_HALF = 5.2                                  # half width of the gap between arms

ARM_Z0, ARM_Z1 = 7.2, 6.3                     # arm lower edge front / rear (local)
LIP_W, LIP_H = 0.7, 1.6                       # lip along the arm's lower outer edge

VIEW = {"azimuth": 45, "elevation": 26}


def prism_xy(pts, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .polyline(pts).close().extrude(z1 - z0))


def prism_yz(pts, x0, x1):
    # polygon given as (y, z) pairs, extruded from x0 to x1
    return (cq.Workplane("YZ").workplane(offset=x0)
            .polyline(pts).close().extrude(x1 - x0))


# plan outline (right half, local coordinates): flank running into the arm
OUTER = [(FR_X, 22.35), (19.4, 23.2), (17.4, 24.4), (15.7, 25.6), (14.1, 27.1),
         (12.8, 28.8), (11.6, 30.9), (10.7, 33.4), (10.25, 36.5), (10.5, 41.9),
         (11.6, 47.3), (12.75, 51.1), (13.7, 54.0)]
INNER = [(10.0, 54.0), (9.3, 51.1), (7.7, 47.3), (6.4, 41.9), (5.5, 36.5),
         (U_HALF, BR_Y1 + 1.2)]


def foot(z0, z1):
    """full plan outline of the lever (both sides in one wire), extruded"""
    m = lambda p: (-p[0], p[1])
    w = (cq.Workplane("XY").workplane(offset=z0)
         .moveTo(-FR_X, FR_Y0).lineTo(FR_X, FR_Y0)
         .lineTo(*OUTER[0])
         .spline(OUTER[1:], includeCurrent=True)
         .lineTo(*INNER[0])
         .spline(INNER[1:], includeCurrent=True)
         .threePointArc((U_HALF - 0.35, BR_Y1 + 0.35), (U_HALF - 1.2, BR_Y1))
         .lineTo(-(U_HALF - 1.2), BR_Y1)
         .threePointArc(m((U_HALF - 0.35, BR_Y1 + 0.35)), m(INNER[-1]))
         .spline([m(p) for p in reversed(INNER[:-1])], includeCurrent=True)
         .lineTo(*m(OUTER[-1]))
         .spline([m(p) for p in reversed(OUTER[:-1])], includeCurrent=True)
         .close())
    return w.extrude(z1 - z0)


FOOT = foot(0.0, 30.0)                        # plan-view limit of the lever

# ======================= tube =======================
box = cq.Workplane("XY").box(BOX_L, BOX_W, BOX_H, centered=(True, True, False))
tube_cut = (cq.Workplane("YZ").workplane(offset=-BOX_L)
            .center(0, BOX_H / 2.0).rect(OPEN_W, OPEN_H).extrude(2 * BOX_L))
box = box.cut(tube_cut)
slot = (cq.Workplane("XY").workplane(offset=-1)
        .rect(SLOT_L, SLOT_W).extrude(WALL_B + 2))
body = box.cut(slot)

# ======================= legs (global) =======================
for s in (-1, 1):
    xa, xb = sorted((s * LEG_X0, s * LEG_X1))
    leg = prism_yz([(BOX_W / 2 - 0.5, 0.0), (LEG_Y1 - 1.2, 0.0), (LEG_Y1, 1.2),
                    (LEG_Y1, LEG_H + 0.5), (13.0, LEG_H + 0.5), (11.2, 9.45),
                    (BOX_W / 2 - 0.5, 9.45)], xa, xb)
    tab = prism_yz([(8.7, BOX_H), (BOX_W / 2, BOX_H), (BOX_W / 2, 9.45),
                    (8.7, 9.45)], xa, xb)
    body = body.union(leg).union(tab)

# ======================= lever (local, untilted) =======================
# thin base plate (front part of the plan outline)
frame = FOOT.intersect(prism_xy([(-30, FR_Y0 - 1), (30, FR_Y0 - 1), (30, BR_Y1),
                                 (-30, BR_Y1)], PL_Z0, PL_Z1))

# raised ring around the central hole
frame = frame.union(cq.Workplane("XY").workplane(offset=PL_Z0)
                    .center(0, HOLE_Y).circle(RING_R).extrude(PL_Z1 + 0.4 - PL_Z0))

# low rib running from the ring towards the right block
frame = frame.union(prism_xy([(RING_R - 0.3, HOLE_Y - 0.2), (BLK_XR + 0.5, HOLE_Y + 0.3),
                              (BLK_XR + 0.5, HOLE_Y + 0.9), (RING_R - 0.3, HOLE_Y + 1.2)],
                             PL_Z0, PL_Z1 + 0.4))

# two rectangular pockets in the plate, open to the front edge
for s in (-1, 1):
    xa, xb = sorted((s * POCK_X0, s * POCK_X1))
    frame = frame.cut(prism_xy([(xa, FR_Y0 - 1), (xb, FR_Y0 - 1), (xb, POCK_Y1),
                                (xa, POCK_Y1)], PL_Z1 - 0.5, PL_Z1 + 2.0))

# ramp + bridge between the arms
bridge = prism_yz([(RAMP_Y0, PL_Z1), (BR_Y0 - 0.6, 10.6), (BR_Y0 + 0.6, BR_Z),
                   (BR_Y1 + 1.0, BR_Z), (BR_Y1 + 1.0, PL_Z0), (RAMP_Y0, PL_Z0)],
                  -BR_X, BR_X)
bridge = bridge.edges("|X").edges(">Z").edges("<Y").fillet(BR_FIL)
frame = frame.union(bridge.intersect(FOOT))

# side blocks, bounded by the flank; their tops rise slightly towards the arms
blk_top = prism_yz([(BLOCK_Y0 - 1.0, 0.0), (BR_Y1 + 3.0, 0.0), (BR_Y1 + 3.0, WALL_TOP + 1.4),
                    (29.0, WALL_TOP + 1.0), (26.5, WALL_TOP + 0.35),
                    (BLOCK_Y0 - 1.0, WALL_TOP + 0.3)], -30.0, 30.0)
blk_l = prism_xy([(-25.0, BLOCK_Y0), (-BLK_XL, BLOCK_Y0), (-BLK_XL + 4.0, BR_Y1),
                  (-BLK_XL + 4.0, BR_Y1 + 2.0), (-25.0, BR_Y1 + 2.0)],
                 PL_Z0, WALL_TOP + 2.0)
frame = frame.union(blk_l.intersect(FOOT).intersect(blk_top))
blk_r = prism_xy([(BLK_XR, BLOCK_Y0), (25.0, BLOCK_Y0), (25.0, BR_Y1 + 2.0),
                  (BLK_XR - 2.5, BR_Y1 + 2.0), (BLK_XR - 2.5, BR_Y1)],
                 PL_Z0, WALL_TOP + 2.0)
frame = frame.union(blk_r.intersect(FOOT).intersect(blk_top.translate((0, 0, 0.2))))

# outer side walls (right one high with sloped front, left one low)
ext_r = prism_xy([(LEG_X0, 14.0), (LEG_X1, 14.0), (LEG_X1, FR_Y0 + 0.5),
                  (LEG_X0, FR_Y0 + 0.5)], 0, 30)
wall_r = prism_yz([(15.0, PL_Z0 + 0.8), (FR_Y0, PL_Z0), (BR_Y1, PL_Z0), (BR_Y1, WALL_TOP),
                   (22.85, WALL_TOP), (19.0, 13.1), (15.0, 11.0)],
                  LEG_X0, LEG_X1)
frame = frame.union(wall_r.intersect(FOOT.union(ext_r)))
ext_l = ext_r.mirror("YZ")
wall_l = prism_yz([(15.0, PL_Z0 + 0.8), (FR_Y0, PL_Z0), (25.0, PL_Z0), (25.0, 9.6), (16.0, 11.4),
                   (15.0, 11.4)], -LEG_X1, -LEG_X0)
frame = frame.union(wall_l.intersect(FOOT.union(ext_l)))

# pins (along x, on the pivot axis) with round knobs at their inner ends
for s in (-1, 1):
    x0 = min(s * PIN_X, s * (LEG_X0 + 0.5))
    frame = frame.union(cq.Workplane("YZ").workplane(offset=x0)
                        .center(PIV_Y, PIV_Z).circle(PIN_R)
                        .extrude(LEG_X0 + 0.5 - PIN_X))
    frame = frame.union(cq.Workplane("XY").workplane(offset=PL_Z0)
                        .center(s * PIN_X, PIV_Y).circle(KNOB_R)
                        .extrude(PIV_Z + PIN_R + 0.15 - PL_Z0))

# arms: side profile (local y, z) cut by a lofted band whose inner face leans
# outwards, so that each arm is thick at its root and thin along its top edge
ARM_PROF = [(BR_Y0 + 1.2, ARM_Z0), (47.5, ARM_Z1),
            (49.4, 7.4), (50.6, 9.5), (51.0, 12.5), (50.2, 15.3), (48.4, 17.1),
            (46.3, 17.6), (43.8, 17.4), (40.5, 16.1), (37.6, 15.0), (33.2, 14.25),
            (BR_Y0 + 1.2, WALL_TOP)]
ARM_OUT = [(12.6, 28.0), (11.3, 31.5), (10.7, 33.4), (10.25, 36.5), (10.5, 41.9),
           (11.6, 47.3), (12.75, 51.1), (13.7, 54.0)]
ARM_IN_B = [(10.0, 54.0), (9.3, 51.1), (7.7, 47.3), (6.4, 41.9), (5.5, 36.5),
            (5.2, 33.5), (4.6, 28.0)]
ARM_IN_T = [(13.1, 54.0), (12.15, 51.1), (11.0, 47.3), (9.9, 41.9), (9.4, 36.5),
            (9.2, 33.5), (9.0, 28.0)]
ARM_LZ0, ARM_LZM, ARM_LZ1 = 5.0, 12.5, 18.5   # loft levels (local): vertical, then leaning


def arm_band_wire(s, inner, z):
    m = lambda p: cq.Vector(s * p[0], p[1], z)
    e1 = cq.Edge.makeSpline([m(p) for p in ARM_OUT])
    e2 = cq.Edge.makeLine(m(ARM_OUT[-1]), m(inner[0]))
    e3 = cq.Edge.makeSpline([m(p) for p in inner])
    e4 = cq.Edge.makeLine(m(inner[-1]), m(ARM_OUT[0]))
    return cq.Wire.assembleEdges([e1, e2, e3, e4])


paddle = (cq.Workplane("YZ").workplane(offset=-25.0)
          .moveTo(*ARM_PROF[0]).lineTo(*ARM_PROF[1])
          .spline(ARM_PROF[2:], includeCurrent=True)
          .close()
          .extrude(50.0))
for s in (-1, 1):
    band = cq.Solid.makeLoft([arm_band_wire(s, ARM_IN_B, ARM_LZ0),
                              arm_band_wire(s, ARM_IN_B, ARM_LZM),
                              arm_band_wire(s, ARM_IN_T, ARM_LZ1)], True)
    arm = paddle.intersect(cq.Workplane("XY").newObject([band]))
    frame = frame.union(arm)
    # lip running along the lower outer edge of the arm
    lip_pts = [cq.Vector(s * x, y, 0) for (x, y) in ARM_OUT[1:]]
    lip_pts_o = [cq.Vector(s * (x + LIP_W), y, 0) for (x, y) in reversed(ARM_OUT[1:])]
    lip_w = cq.Wire.assembleEdges([
        cq.Edge.makeSpline(lip_pts), cq.Edge.makeLine(lip_pts[-1], lip_pts_o[0]),
        cq.Edge.makeSpline(lip_pts_o), cq.Edge.makeLine(lip_pts_o[-1], lip_pts[0])])
    lip_plan = cq.Workplane("XY").newObject([cq.Solid.extrudeLinear(
        cq.Face.makeFromWires(lip_w), cq.Vector(0, 0, 30))])
    lip_side = prism_yz([(BR_Y0 + 1.0, ARM_Z0 - 0.01), (47.5, ARM_Z1 - 0.01),
                         (49.2, 7.3), (47.5, ARM_Z1 + LIP_H),
                         (BR_Y0 + 1.0, ARM_Z0 + LIP_H)], -30.0, 30.0)
    frame = frame.union(lip_plan.intersect(lip_side))

# central hole with a counterbore from below (thin lip)
frame = frame.cut(cq.Workplane("XY").workplane(offset=0.0)
                  .center(0, HOLE_Y).circle(HOLE_R).extrude(30))
frame = frame.cut(cq.Workplane("XY").workplane(offset=0.0)
                  .center(0, HOLE_Y).circle(HOLE_R + 0.6).extrude(PL_Z1 - 0.05))

# tilt the lever about the pin axis
frame = frame.rotate((0, PIV_Y, PIV_Z), (1, PIV_Y, PIV_Z), TILT)

result = body.union(frame)
